import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 10.0            # boss outer diameter
W = 32.5            # plate width (X)
L = 65.0            # plate length (local Y)
T = 3.65            # plate thickness
GAP_L = 3.5         # gap between left and middle plate
GAP_R = 5.2         # gap between middle and right plate (wider)
R_END = 23.5        # radius of the arched ends of the outer plates
R_END_CORNER = 4.5  # small round where arc meets straight side
R_MID_CORNER = 3.4  # corner radius of the middle plate

BOSS_H = 10.9       # boss height above plate top
PITCH = 21.5        # boss pitch along the plate
SEAM_ANG = 80.0     # where the cylinder seam sits (hidden side)
CROSS_LEN = 7.2     # cross recess arm length
CROSS_W = 2.2       # cross recess arm width
CROSS_DEPTH = 3.0   # cross recess depth

TAB_R_OUT = 7.7     # outer radius of the small tabs around each boss
TAB_W = 2.8         # tab width
TAB_H = 2.5         # tab height
TAB_N = 6           # tabs per boss
TAB_START = 30.0    # angle of first tab (deg)

CONN_D = 3.5        # connector rod diameter
CONN_OFF = 16.0     # connector offset from plate centre (local Y)

LUMP_W = 8.3        # gate lump width (X) from the flush -X edge
LUMP_H = 6.55       # gate lump depth below the plate underside
LUMP_Y0 = -8.1      # -Y end of the lump bottom face (local Y)
LUMP_Y1 = 9.1       # +Y end face of the lump (square to the plate)
LUMP_DRAFT = 30.0   # -Y end face leans by this (it is world-vertical)
LUMP_R_BOT_M = 4.0  # round, -Y bottom corner
LUMP_R_BOT_P = 1.6  # round, +Y bottom corner
LUMP_R_BOT_X = 1.6  # round, +X bottom edge
LUMP_FLARE_X = 3.5  # +X side flares out this much at the plate (concave arc)
LUMP_FLARE_H = 4.8  # ... over this height
LUMP_FIL_YM = 1.0   # concave fillet at the -Y end
LUMP_FIL_YP = 2.8   # concave fillet at the +Y end

TILT = 30.0         # tilt of the whole sprue about X (deg)

PLATE_X = [-(W + GAP_L), 0.0, (W + GAP_R)]
GAPS = [GAP_L, GAP_R]


def outer_plate(xc):
    s = R_END - math.sqrt(R_END ** 2 - (W / 2.0) ** 2)  # sagitta of end arc
    yc = L / 2.0 - s
    prof = (
        cq.Workplane("XY")
        .workplane(offset=-T)
        .moveTo(xc - W / 2.0, -yc)
        .lineTo(xc - W / 2.0, yc)
        .threePointArc((xc, L / 2.0), (xc + W / 2.0, yc))
        .lineTo(xc + W / 2.0, -yc)
        .threePointArc((xc, -L / 2.0), (xc - W / 2.0, -yc))
        .close()
        .extrude(T)
    )
    return prof.edges("|Z").fillet(R_END_CORNER)


def middle_plate(xc):
    return (
        cq.Workplane("XY")
        .workplane(offset=-T)
        .center(xc, 0)
        .rect(W, L)
        .extrude(T)
        .edges("|Z")
        .fillet(R_MID_CORNER)
    )


def boss(xc, yc):
    cyl = cq.Solid.makeCylinder(D / 2.0, BOSS_H, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1))
    cyl = cyl.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), SEAM_ANG)
    b = cq.Workplane("XY").add(cyl)
    # radial tabs at the foot of the boss
    r_in = D / 2.0 - 0.6
    tab_len = TAB_R_OUT - r_in
    rm = r_in + tab_len / 2.0
    for k in range(TAB_N):
        ang = TAB_START + k * 360.0 / TAB_N
        a = math.radians(ang)
        tab = (
            cq.Workplane("XY")
            .box(tab_len, TAB_W, TAB_H, centered=(True, True, False))
            .rotate((0, 0, 0), (0, 0, 1), ang)
            .translate((rm * math.cos(a), rm * math.sin(a), 0))
        )
        b = b.union(tab)
    # cross recess on top
    cross = (
        cq.Workplane("XY")
        .workplane(offset=BOSS_H - CROSS_DEPTH)
        .rect(CROSS_LEN, CROSS_W)
        .extrude(CROSS_DEPTH + 1)
        .union(
            cq.Workplane("XY")
            .workplane(offset=BOSS_H - CROSS_DEPTH)
            .rect(CROSS_W, CROSS_LEN)
            .extrude(CROSS_DEPTH + 1)
        )
    )
    return b.cut(cross).translate((xc, yc, 0))


def rounded_profile(wp, pts, radii):
    """Closed 2D outline through pts with a tangent arc of radii[i] at vertex i."""
    n = len(pts)
    corners = []
    for i in range(n):
        p, pa, pb, r = pts[i], pts[i - 1], pts[(i + 1) % n], radii[i]
        if r <= 0:
            corners.append((p, p, None))
            continue
        ux, uy = pa[0] - p[0], pa[1] - p[1]
        la = math.hypot(ux, uy)
        ux, uy = ux / la, uy / la
        vx, vy = pb[0] - p[0], pb[1] - p[1]
        lb = math.hypot(vx, vy)
        vx, vy = vx / lb, vy / lb
        ang = math.acos(max(-1.0, min(1.0, ux * vx + uy * vy)))
        d = r / math.tan(ang / 2.0)
        bx, by = ux + vx, uy + vy
        bl = math.hypot(bx, by)
        bx, by = bx / bl, by / bl
        dc = r / math.sin(ang / 2.0)
        mid = (p[0] + bx * (dc - r), p[1] + by * (dc - r))
        corners.append(((p[0] + ux * d, p[1] + uy * d), (p[0] + vx * d, p[1] + vy * d), mid))
    wp = wp.moveTo(*corners[0][1])
    for k in range(1, n + 1):
        t1, t2, mid = corners[k % n]
        wp = wp.lineTo(*t1)
        if mid is not None:
            wp = wp.threePointArc(mid, t2)
    return wp.close()


def middle_with_gate(xc):
    """Middle plate with the moulding gate lump on its underside (-X edge)."""
    plate = middle_plate(xc)
    x0 = xc - W / 2.0
    zt = -T
    zb = -T - LUMP_H
    tn = math.tan(math.radians(LUMP_DRAFT))
    ym_top = LUMP_Y0 - LUMP_H * tn
    e = 1.0  # overlap into the plate
    # side profile (local Y-Z), pushed along X
    ya = ym_top - LUMP_FIL_YM - e
    yb = LUMP_Y1 + LUMP_FIL_YP + e
    ypts = [
        (ya, zt + e),
        (ya, zt),
        (ym_top, zt),
        (LUMP_Y0, zb),
        (LUMP_Y1, zb),
        (LUMP_Y1, zt),
        (yb, zt),
        (yb, zt + e),
    ]
    yrad = [0, 0, LUMP_FIL_YM, LUMP_R_BOT_M, LUMP_R_BOT_P, LUMP_FIL_YP, 0, 0]
    side = rounded_profile(cq.Workplane("YZ").workplane(offset=x0 - e), ypts, yrad).extrude(
        LUMP_W + LUMP_FLARE_X + 3 * e
    )
    # cross profile (local X-Z): flush -X side, +X side flaring into the plate
    xr = x0 + LUMP_W
    rb = LUMP_R_BOT_X
    a, h = LUMP_FLARE_X, LUMP_FLARE_H
    rf = (a * a + h * h) / (2.0 * a)          # flare arc radius (tangent to the +X side)
    cxf, czf = xr + rf, zt - h                # its centre
    ang_top = math.atan2(zt - czf, (xr + a) - cxf)
    ang_mid = 0.5 * (math.pi + ang_top)
    mid_f = (cxf + rf * math.cos(ang_mid), czf + rf * math.sin(ang_mid))
    s2 = math.sqrt(0.5)
    cross = (
        cq.Workplane("XZ")
        .workplane(offset=-L / 2.0)
        .moveTo(x0, zt + e)
        .lineTo(x0, zb)
        .lineTo(xr - rb, zb)
        .threePointArc((xr - rb + rb * s2, zb + rb - rb * s2), (xr, zb + rb))
        .lineTo(xr, czf)
        .threePointArc(mid_f, (xr + a, zt))
        .lineTo(xr + a + e, zt)
        .lineTo(xr + a + e, zt + e)
        .close()
        .extrude(L)
    )
    lump = side.intersect(cross)
    return plate.union(lump)


# ---------------- build in plate-local frame ----------------
part = outer_plate(PLATE_X[0])
part = part.union(middle_with_gate(PLATE_X[1]))
part = part.union(outer_plate(PLATE_X[2]))

for xc in PLATE_X:
    for j in (-1, 0, 1):
        part = part.union(boss(xc, j * PITCH))

# connector rods between plates
for i in range(2):
    xa = PLATE_X[i] + W / 2.0 - 0.5
    span = GAPS[i] + 1.0
    for yc in (-CONN_OFF, 0.0, CONN_OFF):
        rod = (
            cq.Workplane("YZ")
            .workplane(offset=xa)
            .center(yc, -T / 2.0)
            .circle(CONN_D / 2.0)
            .extrude(span)
        )
        part = part.union(rod)

# tilt the whole sprue about X so the plates slope down toward +Y
result = part.rotate((0, 0, 0), (1, 0, 0), -TILT)

VIEW = {"azimuth": 45, "elevation": 26}
